import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 200.0          # overall length along X
W = 151.0          # overall depth along Y
H = 23.5           # overall height along Z
WALL = 2.4         # side wall thickness (at the open bottom)
WALL_XP = 3.4      # the +X (connector) wall is thicker
TOP = 2.4          # top plate thickness

# display window in the top plate (margins from outer edges)
M_XN = 6.0         # -X margin
M_XP = 9.7         # +X margin
M_YP = 21.1        # +Y (back) margin
M_YN = 25.8        # -Y (front) margin

# inner step on the -X wall (upper part of the wall is thinner)
STEP_Z = 12.6      # height of the up-facing ledge
STEP_D = 1.2       # how far the upper wall is recessed

# corner block under the top plate at the (-X,+Y) inside corner
BLK_X = 9.5        # size along X (from the recessed wall face)
BLK_Y = 11.4       # size along Y (from the inner +Y wall face)
BLK_Z0 = 11.0      # bottom of block

# recess in the lower inside of the +X wall (behind the connectors)
RX_Z1 = 9.1
RX_D = 1.0
RX_Y0 = -60.8
RX_Y1 = 60.8

# ventilation holes through both X walls
HOLE_D = 3.2
HOLE_N = 12
HOLE_PITCH = 5.9
HOLE_Y0 = -W / 2 + 16.8    # first hole centre (Y)
HOLE_Z = 7.8

# small rectangular slots on +X wall
SLOT_W = 8.9
SLOT_H = 3.4
SLOT_Z = 7.8
SLOT_YS = [15.2, 28.2]

# port (recess + through opening) on +X wall
PORT_Y = 49.7
REC_W, REC_Z0, REC_Z1, REC_D = 22.8, 0.6, 11.8, 0.8
PORT_W, PORT_Z0, PORT_Z1 = 17.7, 2.7, 9.4

EPS = 0.01
ZC = H - TOP        # underside of the top plate

# ---------------- body ----------------
body = cq.Workplane("XY").box(L, W, H, centered=(True, True, False))

# open cavity from below
ix0, ix1 = -L / 2 + WALL, L / 2 - WALL_XP
iy0, iy1 = -W / 2 + WALL, W / 2 - WALL
cav = (cq.Workplane("XY").box(ix1 - ix0, iy1 - iy0, ZC + EPS, centered=False)
       .translate((ix0, iy0, -EPS)))
body = body.cut(cav)

# upper recess of the -X wall (creates an up-facing ledge)
rec_xn = (cq.Workplane("XY")
          .box(STEP_D + EPS, iy1 - iy0, ZC - STEP_Z, centered=False)
          .translate((ix0 - STEP_D, iy0, STEP_Z)))
body = body.cut(rec_xn)

# corner blocks under the top plate at (-X,+Y) and, rotated 180 deg, at (+X,-Y)
blk = (cq.Workplane("XY")
       .box(BLK_X, BLK_Y, ZC - BLK_Z0 + EPS, centered=False)
       .translate((ix0 - STEP_D, iy1 - BLK_Y, BLK_Z0)))
body = body.union(blk)
bx_conv = -(ix0 - STEP_D + BLK_X)      # convex corner x of the rotated copy
blk2 = (cq.Workplane("XY")
        .box(ix1 + EPS - bx_conv, BLK_Y, ZC - BLK_Z0 + EPS, centered=False)
        .translate((bx_conv, iy0, BLK_Z0)))
body = body.union(blk2)

# lower recess inside the +X wall
rec_xp = (cq.Workplane("XY")
          .box(RX_D + EPS, RX_Y1 - RX_Y0, RX_Z1 + EPS, centered=False)
          .translate((ix1 - EPS, RX_Y0, -EPS)))
body = body.cut(rec_xp)

# window through the top plate
win_x0 = -L / 2 + M_XN
win_x1 = L / 2 - M_XP
win_y0 = -W / 2 + M_YN
win_y1 = W / 2 - M_YP
window = (cq.Workplane("XY")
          .center((win_x0 + win_x1) / 2, (win_y0 + win_y1) / 2)
          .rect(win_x1 - win_x0, win_y1 - win_y0)
          .extrude(H + 2).translate((0, 0, -1)))
body = body.cut(window)

# holes through both X walls
pts = [(HOLE_Y0 + i * HOLE_PITCH, HOLE_Z) for i in range(HOLE_N)]
holes = (cq.Workplane("YZ").workplane(offset=-L / 2 - 1)
         .pushPoints(pts).circle(HOLE_D / 2).extrude(L + 2))
body = body.cut(holes)

# slots on +X wall
for ys in SLOT_YS:
    s = (cq.Workplane("YZ").workplane(offset=L / 2 - WALL_XP - 1)
         .center(ys, SLOT_Z).rect(SLOT_W, SLOT_H).extrude(WALL_XP + 2))
    body = body.cut(s)

# port recess and through opening on +X wall
rec = (cq.Workplane("YZ").workplane(offset=L / 2 - REC_D)
       .center(PORT_Y, (REC_Z0 + REC_Z1) / 2)
       .rect(REC_W, REC_Z1 - REC_Z0).extrude(REC_D + 1))
body = body.cut(rec)
port = (cq.Workplane("YZ").workplane(offset=L / 2 - WALL_XP - 1)
        .center(PORT_Y, (PORT_Z0 + PORT_Z1) / 2)
        .rect(PORT_W, PORT_Z1 - PORT_Z0).extrude(WALL_XP + 2))
body = body.cut(port)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
